import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# body frame: face looks along +X, shoulders along Y, base plane z = 0
SH_HALF = 62.0            # half shoulder span (Y)
SH_DEPTH_HALF = 26.0      # half depth of base (X)
SH_TOP = 21.0             # shoulder/torso height at the centre
TORSO_DROP = 10.0         # torso ellipsoid centre below the base plane

BACK_CX = -6.0            # upper-back / trapezius mound
BACK_RX, BACK_RY = 22.0, 28.0
BACK_WALL = 15.0          # height of the steep part of the back
BACK_CAP = 12.0           # rounded cap on top of the back mound

TORSO_BLEND_R = 6.0       # blend of the back mound into the shoulders

NECK_RX, NECK_RY, NECK_TOP = 18.5, 17.0, 62.0
NECK_BLEND_R = 5.0        # blend of the neck into the shoulders

CRANIUM_C = (-7.9, 0.0, 59.7)         # head dome (hair + face mass)
CRANIUM_AX = (36.7, 36.0, 43.0)
CRANIUM_TILT = 28.9                   # dome leans forward
CRANIUM_BOTTOM = 45.0
CROWN_C = (-10.0, 0.0, 74.5)          # fuller, flatter crown at the back
CROWN_AX = (28.0, 32.0, 26.0)

FACE_C = (15.4, 0.0, 62.4)             # face mask (forehead, cheeks, jaw)
FACE_AX = (18.0, 21.0, 30.0)
FACE_TILT = -18.9                      # face looks slightly up

# bob flare: half-width (Y) of the hair bell against height, built from arcs
BELL_TOP = 68.0
BELL_TOP_R = 30.0
BELL_ARCS = [((40.5, 60.0), (45.0, 46.0)),
             ((43.5, 36.0), (35.0, 28.5)),
             ((27.0, 25.5), (16.0, 24.5))]
BELL_BOTTOM = 24.5
BELL_CX, BELL_CY = 0.0, 0.0           # bell centre
BELL_SX_BACK = 1.02                   # depth/width ratio behind the centre
BELL_SX_FRONT = 0.40                  # depth/width ratio in front (face side)
BELL_TURN = 9.0                       # bob hangs square to the shoulders
HAIR_BLEND_R = 8.0        # blend between the dome and the bob flare

NOSE_C = (33.0, 0.0, 62.0)
NOSE_AX = (4.5, 4.0, 7.0)
NOSE_TILT = FACE_TILT
CHIN_C = (28.5, 0.0, 40.0)
CHIN_AX = (5.5, 8.0, 5.5)
NAPE_C = (-24.0, 0.0, 31.0)            # hair hanging down over the nape
NAPE_AX = (13.0, 30.0, 8.0)
LOCK_C = (8.0, 29.0, 54.0)             # hair curtain hanging at the +Y cheek
LOCK_AX = (20.0, 11.0, 22.0)
CURL_C = (18.0, 27.0, 36.0)            # its end curling forward along the jaw
CURL_AX = (18.0, 9.0, 8.0)
CURL_TURN = -15.0

TORSO_TWIST = -14.0       # shoulders turned about Z
HEAD_TWIST = -9.0         # head turned about Z

VIEW = {"azimuth": 45, "elevation": 26}


def scaled(solid, sx=1.0, sy=1.0, sz=1.0, tx=0.0, ty=0.0, tz=0.0):
    m = cq.Matrix([[sx, 0, 0, tx], [0, sy, 0, ty], [0, 0, sz, tz]])
    return solid.transformGeometry(m)


def ellipsoid(c, ax, tilt_y=0.0, turn_z=0.0):
    s = cq.Solid.makeSphere(1.0, angleDegrees1=-90, angleDegrees2=90)
    e = scaled(s, ax[0], ax[1], ax[2])
    if tilt_y:
        e = e.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), tilt_y)
    if turn_z:
        e = e.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), turn_z)
    return e.translate(cq.Vector(*c))


def box(x0, x1, y0, y1, z0, z1):
    return cq.Solid.makeBox(x1 - x0, y1 - y0, z1 - z0, cq.Vector(x0, y0, z0))


def above(z0):
    return box(-150, 150, -150, 150, z0, z0 + 300)


# ---------------- torso / shoulders ----------------
_k = math.sqrt(1.0 - (TORSO_DROP / (SH_TOP + TORSO_DROP)) ** 2)
torso = ellipsoid((0, 0, -TORSO_DROP),
                  (SH_DEPTH_HALF / _k, SH_HALF / _k, SH_TOP + TORSO_DROP))
back_wall = (
    cq.Workplane("XY").center(BACK_CX, 0).ellipse(BACK_RX, BACK_RY)
    .extrude(BACK_WALL).val()
)
back_cap = ellipsoid((BACK_CX, 0, BACK_WALL), (BACK_RX, BACK_RY, BACK_CAP))
torso = torso.fuse(back_wall).fuse(back_cap).intersect(above(0.0))


def _span(e):
    b = e.BoundingBox()
    return b.xmax - b.xmin, b.ymax - b.ymin, b.zmax - b.zmin


blend = [e for e in torso.Edges() if _span(e)[1] > 5.0 and _span(e)[2] > 2.0]
try:
    torso = torso.fillet(TORSO_BLEND_R, blend)
except Exception:
    pass

neck = cq.Workplane("XY").ellipse(NECK_RX, NECK_RY).extrude(NECK_TOP).val()

# ---------------- head ----------------
cranium = ellipsoid(CRANIUM_C, CRANIUM_AX, CRANIUM_TILT).intersect(above(CRANIUM_BOTTOM))
face = ellipsoid(FACE_C, FACE_AX, FACE_TILT)

wp = cq.Workplane("XZ").moveTo(0, BELL_TOP).lineTo(BELL_TOP_R, BELL_TOP)
for mid, end in BELL_ARCS:
    wp = wp.threePointArc(mid, end)
bell = wp.lineTo(0, BELL_BOTTOM).close().revolve(360, (0, 0, 0), (0, 1, 0)).val()
bell_f = scaled(bell.intersect(box(0, 100, -100, 100, 0, 200)), BELL_SX_FRONT)
bell_b = scaled(bell.intersect(box(-100, 0, -100, 100, 0, 200)), BELL_SX_BACK)
bell = bell_f.fuse(bell_b).clean()
bell = bell.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), BELL_TURN)
bell = bell.translate(cq.Vector(BELL_CX, BELL_CY, 0))

crown = ellipsoid(CROWN_C, CROWN_AX)
nape = ellipsoid(NAPE_C, NAPE_AX)
hair = cranium.fuse(crown).fuse(bell)
ring = [e for e in hair.Edges()
        if e.Length() > 100.0
        and e.BoundingBox().zmax - e.BoundingBox().zmin > 5.0]
try:
    hair = hair.fillet(HAIR_BLEND_R, ring)
except Exception:
    pass

nose = ellipsoid(NOSE_C, NOSE_AX, NOSE_TILT)
chin = ellipsoid(CHIN_C, CHIN_AX)
curl = ellipsoid(CURL_C, CURL_AX, 0.0, CURL_TURN)
lock = ellipsoid(LOCK_C, LOCK_AX, 0.0, CURL_TURN)

head = hair.fuse(face).fuse(nose).fuse(chin).fuse(lock).fuse(curl).fuse(nape)

ZAXIS = (cq.Vector(0, 0, 0), cq.Vector(0, 0, 1))
torso = torso.rotate(*ZAXIS, TORSO_TWIST)
neck = neck.rotate(*ZAXIS, HEAD_TWIST)
head = head.rotate(*ZAXIS, HEAD_TWIST)
body = torso.fuse(neck)
collar = [e for e in body.Edges()
          if e.BoundingBox().zmax < 40.0 and e.BoundingBox().zmin > 5.0
          and max(abs(e.BoundingBox().xmin), abs(e.BoundingBox().xmax),
                  abs(e.BoundingBox().ymin), abs(e.BoundingBox().ymax)) < 25.0
          and e.Length() > 10.0]
try:
    body = body.fillet(NECK_BLEND_R, collar)
except Exception:
    pass
body = body.fuse(head).clean()

result = cq.Workplane("XY").add(body)
